import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
AF = 35.0            # across-flats of the octagonal bar
L = 65.0             # length of the bar (along Y)
SLOT_D = 12.55       # diameter of the double-D through bore
SLOT_W = 7.46        # width across the two flats of the bore
BUMP_BASE_D = 9.65   # footprint diameter of each spherical dome
BUMP_H = 2.45        # dome height above its face
BUMP_PITCH = 21.65  # axial pitch of the three code positions

# Each face carries a unique 3-bit code of domes at axial positions A, B, C
# (A nearest the front end, -Y).  Faces indexed by normal angle in XZ plane,
# 0 deg = +X, 90 deg = +Z.
CODES = {
    0: (0, 1, 0),
    45: (1, 0, 0),
    90: (0, 0, 0),
    135: (1, 1, 1),
    180: (0, 1, 1),
    225: (1, 0, 1),
    270: (0, 0, 1),
    315: (1, 1, 0),
}

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- body: regular octagon prism along Y ----------------
r_corner = (AF / 2.0) / math.cos(math.radians(22.5))
pts = [
    (r_corner * math.cos(math.radians(22.5 + 45 * i)),
     r_corner * math.sin(math.radians(22.5 + 45 * i)))
    for i in range(8)
]
# XZ workplane: local x = +X, local y = +Z, extrusion toward -Y
body = (
    cq.Workplane("XZ", origin=(0, L / 2.0, 0))
    .polyline(pts).close()
    .extrude(L)
)

# ---------------- spherical code domes ----------------
a = BUMP_BASE_D / 2.0
R_sph = (a * a + BUMP_H * BUMP_H) / (2.0 * BUMP_H)
center_r = AF / 2.0 - (R_sph - BUMP_H)
axial = [-BUMP_PITCH, 0.0, BUMP_PITCH]   # A, B, C along +Y

for ang, code in CODES.items():
    c = math.cos(math.radians(ang))
    s = math.sin(math.radians(ang))
    for bit, y in zip(code, axial):
        if not bit:
            continue
        # sphere poles along the bar axis and its seam meridian turned to
        # face inward, so the exposed dome is a single seamless patch
        sph = (
            cq.Workplane("XY").sphere(R_sph)
            .rotate((0, 0, 0), (1, 0, 0), 90)
            .rotate((0, 0, 0), (0, 1, 0), 180 - ang)
            .translate((center_r * c, y, center_r * s))
        )
        body = body.union(sph)

# ---------------- double-D through bore ----------------
bore = (
    cq.Workplane("XZ", origin=(0, L / 2.0 + 1.0, 0))
    .circle(SLOT_D / 2.0)
    .extrude(L + 2.0)
)
keep = (
    cq.Workplane("XZ", origin=(0, L / 2.0 + 1.0, 0))
    .rect(SLOT_W, SLOT_D + 2.0)
    .extrude(L + 2.0)
)
bore = bore.intersect(keep)
body = body.cut(bore)

result = body
